import cadquery as cq
import math

# ================= driving dimensions (mm) =================
T = 5.5                  # plate thickness (both plates)
EDGE_R = 2.4             # edge rounding of the plates

# ---- lower (round) plate, centred on the origin, underside at Z=0 ----
LD = 212.5               # diameter
WIN_X = 79.4             # central window width (X)
WIN_Y0, WIN_Y1 = -5.6, 47.4
LSLOT_X, LSLOT_W = 69.6, 14.8          # long side slots
LSLOT_Y0, LSLOT_Y1 = -12.5, 52.4
SSLOT_W, SSLOT_L = 8.8, 17.4           # small rectangular slots
SSLOTS = [(62.2, -36.9), (31.8, -72.4)]   # mirrored in X
HOLE_D = 5.5
SMALL_HOLE_D = 3.5
LHOLES = [(90.0, -0.3), (71.1, -53.2), (69.2, -69.6), (13.3, -96.7), (24.5, -21.0),
          (68.7, 68.1), (13.3, 87.2)]          # mirrored in X
LHOLES_SMALL = [(50.9, 2.9), (51.1, 36.7)]    # mirrored in X
WHEEL_C = (141.25, -55.1)              # wheel clearance scallops (mirrored)
WHEEL_R = 57.8
# ---- walls standing on the lower plate ----
WALL_X = 17.7            # wall centre offset from Y axis
WALL_T = 7.4
WALL_Y0, WALL_Y1 = -80.7, -27.2
WALL_H = 24.9            # height above the lower plate
WALL_R = 1.2             # wall edge rounding

# ---- upper (rectangular) plate ----
UW = 193.8               # width (X)
UL = 229.6               # length (Y)
UBW = 106.4              # width of the narrowed back edge
U_DX, U_DY = -1.8, 15.0  # plate centre offset from lower plate centre
U_Z = 79.7               # underside height of the upper plate
GRID_DX, GRID_DY = 1.0, 0.5   # small offset of the slot grid
GRID_COLS = [-34.6, 0.0, 34.6]
GRID_ROWS = [70.8, 28.7, -17.2, -62.8]
GSLOT_L, GSLOT_W = 17.5, 9.3
SIDE_SLOT_X, SIDE_SLOT_W = 80.2, 9.2
SLOT2_END_OUT, SLOT2_END_IN = -33.7, -45.0   # slanted front end of the front side slots
UHOLES = [(68.7, 69.2), (68.7, -67.7), (89.6, 0.6)]          # mirrored in X
# front bow-tie flap
FLAP_TOP, FLAP_TIP, FLAP_D, FLAP_T = 66.2, 51.8, 17.6, 2.9
FLAP_IN = 1.4            # set-back of the front flap from the front edge
# back bow-tie flap (shallower, mostly hidden behind the front one)
BFLAP_TOP, BFLAP_TIP, BFLAP_D, BFLAP_T = 67.0, 52.0, 8.7, 2.9
BFLAP_IN = 3.2

hw, hl, bw = UW / 2.0, UL / 2.0, UBW / 2.0
# concave transition from the narrow back edge to the side edge (right-hand side, mirrored)
BACK_CURVE = [(56.6, 106.9), (63.6, 96.0), (76.2, 83.4), (86.5, 75.8), (hw, 69.5)]


def mirror_pts(pts):
    out = []
    for x, y in pts:
        out.append((x, y))
        out.append((-x, y))
    return out


def prism(pts, z0, h):
    return cq.Workplane("XY").polyline(pts).close().extrude(h).translate((0, 0, z0))


# ================= upper plate =================
upper = (cq.Workplane("XY")
         .moveTo(-bw, hl)
         .lineTo(bw, hl)
         .spline([(x, y) for x, y in BACK_CURVE], includeCurrent=True)
         .lineTo(hw, -45.0)
         .lineTo(77.0, -61.4)
         .lineTo(77.0, -66.0)
         .lineTo(82.5, -68.0)
         .lineTo(hw, -102.7)
         .lineTo(hw, -hl)
         .lineTo(-hw, -hl)
         .lineTo(-hw, -102.7)
         .lineTo(-82.5, -68.0)
         .lineTo(-77.0, -66.0)
         .lineTo(-77.0, -61.4)
         .lineTo(-hw, -45.0)
         .lineTo(-hw, BACK_CURVE[-1][1])
         .spline([(-x, y) for x, y in reversed(BACK_CURVE[:-1])] + [(-bw, hl)], includeCurrent=True)
         .close()
         .extrude(T))
# round the straight front/back/side edges and the right-hand notch edge (hemmed look)
ROLL_A, ROLL_B = (77.0, -61.4), (hw, -45.0)
_roll_mid = ((ROLL_A[0] + ROLL_B[0]) / 2.0, (ROLL_A[1] + ROLL_B[1]) / 2.0)


def _round_edge(e):
    d = e.endPoint() - e.startPoint()
    if abs(d.z) > 1e-6:
        return False
    if abs(d.x) < 1e-6 or abs(d.y) < 1e-6:
        return True
    c = e.Center()
    return abs(c.x - _roll_mid[0]) < 1.0 and abs(c.y - _roll_mid[1]) < 1.0


upper = upper.newObject([e for e in upper.edges().vals()
                         if e.geomType() == "LINE" and _round_edge(e)]).fillet(EDGE_R)

ucut = []
for x in GRID_COLS:
    for y in GRID_ROWS:
        ucut.append(cq.Workplane("XY").center(x + GRID_DX, y + GRID_DY).slot2D(GSLOT_L, GSLOT_W, 90).extrude(3 * T).translate((0, 0, -T)))
for sx in (-1, 1):
    ucut.append(cq.Workplane("XY").center(sx * SIDE_SLOT_X, 36.9).slot2D(60.8, SIDE_SLOT_W, 90)
                .extrude(3 * T).translate((0, 0, -T)))
    # front side slot: rounded back end, front end cut on a slant
    ucut.append(cq.Workplane("XY").center(sx * SIDE_SLOT_X, -17.0).slot2D(24.2, SIDE_SLOT_W, 90)
                .extrude(3 * T).translate((0, 0, -T)))
    xo, xi = sx * (SIDE_SLOT_X + SIDE_SLOT_W / 2), sx * (SIDE_SLOT_X - SIDE_SLOT_W / 2)
    ucut.append(prism([(xi, -20.0), (xo, -20.0), (xo, SLOT2_END_OUT), (xi, SLOT2_END_IN)], -T, 3 * T))
    # L-shaped slot at the front corner
    lpath = (cq.Workplane("XY").moveTo(sx * 80.15, -92.35).lineTo(sx * 80.15, -105.05)
             .lineTo(sx * 66.35, -105.05))
    ucut.append(lpath.offset2D(4.65).extrude(3 * T).translate((0, 0, -T)))
ucut.append(cq.Workplane("XY").pushPoints(mirror_pts(UHOLES)).circle(2.8).extrude(3 * T).translate((0, 0, -T)))
for c in ucut:
    upper = upper.cut(c)

# front bow-tie flap (two triangles hanging under the front edge)
def bowtie(top, tip, depth, thick, y0):
    """two triangular tabs meeting at the centre line, hanging below Z=0, from y0 to y0+thick"""
    return (cq.Workplane("XZ")
            .polyline([(-top, 0.6), (0, 0.6), (-tip, -depth)]).close()
            .polyline([(top, 0.6), (0, 0.6), (tip, -depth)]).close()
            .extrude(-thick)
            .translate((0, y0, 0)))


flap = bowtie(FLAP_TOP, FLAP_TIP, FLAP_D, FLAP_T, -hl + FLAP_IN)
bflap = bowtie(BFLAP_TOP, BFLAP_TIP, BFLAP_D, BFLAP_T, hl - BFLAP_IN - BFLAP_T)
upper = upper.union(flap).union(bflap)
upper = upper.translate((U_DX, U_DY, U_Z))

# ================= lower plate =================
# disk with a full-round rim (revolved profile)
rim_prof = (cq.Workplane("XZ").moveTo(0, 0).lineTo(LD / 2.0 - T / 2.0, 0)
            .threePointArc((LD / 2.0, T / 2.0), (LD / 2.0 - T / 2.0, T)).lineTo(0, T).close())
lower = rim_prof.revolve(360, (0, 0, 0), (0, 1, 0))
# wheel clearance scallops with rounded edges
for sx in (-1, 1):
    lower = lower.cut(cq.Workplane("XY").center(sx * WHEEL_C[0], WHEEL_C[1]).circle(WHEEL_R)
                      .extrude(3 * T).translate((0, 0, -T)))


def _is_scallop_edge(e):
    try:
        c = e.arcCenter()
    except Exception:
        return False
    return abs(abs(c.x) - WHEEL_C[0]) < 0.5 and abs(c.y - WHEEL_C[1]) < 0.5


lower = lower.newObject([e for e in lower.edges().vals() if _is_scallop_edge(e)]).fillet(EDGE_R)
# hook notches at the front and V notches at the back (mirrored), cut with sharp edges
NA, NL, NR, NM = (62.2, -76.7), (44.3, -98.3), (34.4, -91.1), (41.5, -96.9)
for sx in (-1, 1):
    lx = NA[0] + 1.15 * (NL[0] - NA[0]); ly = NA[1] + 1.15 * (NL[1] - NA[1])
    mx = NR[0] + 1.3 * (NM[0] - NR[0]); my = NR[1] + 1.3 * (NM[1] - NR[1])
    front_notch = [(sx * NA[0], NA[1]), (sx * lx, ly), (sx * mx, my), (sx * NR[0], NR[1])]
    lower = lower.cut(prism(front_notch, -T, 3 * T))
    back_notch = [(sx * 36.0, 101.5), (sx * 57.7, 77.9), (sx * 76.0, 77.9), (sx * 76.0, 101.5)]
    lower = lower.cut(prism(back_notch, -T, 3 * T))

lcut = []
lcut.append(cq.Workplane("XY").center(0, (WIN_Y0 + WIN_Y1) / 2).rect(WIN_X, WIN_Y1 - WIN_Y0))
lcut.append(cq.Workplane("XY").pushPoints([(LSLOT_X, (LSLOT_Y0 + LSLOT_Y1) / 2),
                                            (-LSLOT_X, (LSLOT_Y0 + LSLOT_Y1) / 2)])
            .rect(LSLOT_W, LSLOT_Y1 - LSLOT_Y0))
lcut.append(cq.Workplane("XY").pushPoints(mirror_pts(SSLOTS)).rect(SSLOT_W, SSLOT_L))
lcut.append(cq.Workplane("XY").pushPoints(mirror_pts(LHOLES) + [(0.0, -33.8)]).circle(HOLE_D / 2))
lcut.append(cq.Workplane("XY").pushPoints(mirror_pts(LHOLES_SMALL)).circle(SMALL_HOLE_D / 2))
for c in lcut:
    lower = lower.cut(c.extrude(3 * T).translate((0, 0, -T)))

walls = (cq.Workplane("XY")
         .pushPoints([(-WALL_X, (WALL_Y0 + WALL_Y1) / 2), (WALL_X, (WALL_Y0 + WALL_Y1) / 2)])
         .rect(WALL_T, WALL_Y1 - WALL_Y0).extrude(WALL_H + 1.0)
         .edges("|Z").fillet(WALL_R)
         .faces(">Z").edges().fillet(WALL_R)
         .translate((0, 0, T - 1.0)))
lower = lower.union(walls)

result = upper.union(lower)
